import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
TOTAL_LEN = 57.0        # overall length along X
COIN_D = 23.4           # coin disc diameter
HANDLE_W = 16.1         # handle width
THK = 2.0               # plate thickness
NECK_FILLET = 5.0       # concave fillet radius, handle -> coin
HOLE_D = 4.0            # key-ring hole diameter
HOLE_X = 4.0            # hole centre from left end

TEXT_H = 0.35           # raised lettering height
TEXT_FILLET = 0.18      # rounding of the letter top edges
STROKE = 1.2            # letter stroke width
HEAVY = 1.35            # width of the diagonal strokes (N, Y)
CAP = 2.6 - STROKE / 2  # half letter height measured to stroke centre
C1_X = 27.98            # centre of first "C"
C_PITCH = 4.67          # spacing of the two "C"s
C_RX, C_RY = 1.85, 2.15 # C centre-line semi-axes (round letters overshoot)
C_OPEN = 45.0           # half opening angle of the "C"
Y_ARM_TOP = 2.95        # top of the "Y" arms (above cap height, like the target)

LOGO_R = 7.8            # logo outer radius
LOGO_DEPTH = 0.45       # logo pocket depth
LOGO_DX = 0.45          # logo centre offset from coin centre
LOGO_DY = -0.1

coin_r = COIN_D / 2.0
coin_x = TOTAL_LEN - coin_r
hw = HANDLE_W / 2.0
end_x = hw              # centre of the handle's rounded end

# ---------------- base plate ----------------
coin = cq.Workplane("XY").center(coin_x, 0).circle(coin_r).extrude(THK)
handle = (
    cq.Workplane("XY")
    .center((end_x + coin_x) / 2.0, 0)
    .slot2D(coin_x - end_x + 2 * hw, HANDLE_W)
    .extrude(THK)
)
plate = coin.union(handle)

# concave fillet between handle and coin (vertical edges at the neck)
x_int = coin_x - math.sqrt(coin_r ** 2 - hw ** 2)
plate = plate.edges("|Z").edges(
    cq.selectors.BoxSelector((x_int - 0.5, -hw - 0.5, -1.0), (x_int + 0.5, hw + 0.5, THK + 1.0))
).fillet(NECK_FILLET)

# key-ring hole
plate = plate.cut(
    cq.Workplane("XY").center(HOLE_X, 0).circle(HOLE_D / 2.0).extrude(THK)
)

# ---------------- raised lettering "NYBICC" ----------------
def stroke_face(wire, width=STROKE):
    """2D face of a pen stroke of the given width (round caps) along a wire."""
    if len(wire.Edges()) == 1 and wire.Edges()[0].geomType() == "LINE":
        vs = wire.Vertices()
        p0, p1 = vs[0].toTuple(), vs[1].toTuple()
        L = math.hypot(p1[0] - p0[0], p1[1] - p0[1])
        ang = math.degrees(math.atan2(p1[1] - p0[1], p1[0] - p0[0]))
        w = (
            cq.Workplane("XY")
            .center((p0[0] + p1[0]) / 2.0, (p0[1] + p1[1]) / 2.0)
            .slot2D(L + width, width, ang)
            .val()
        )
        return cq.Face.makeFromWires(w)
    offs = wire.offset2D(width / 2.0, "arc")
    return cq.Face.makeFromWires(offs[0])


def poly(pts):
    return cq.Wire.makePolygon([cq.Vector(x, y, 0) for x, y in pts])


def c_wire(cx, cy, rx, ry, a0):
    """Centre-line of a tall "C": two arcs of radius rx joined by a short
    vertical run, so the letter is 2*ry tall and opens by +-a0 degrees."""
    V = cq.Vector
    d = ry - rx
    t = math.radians(a0)
    p_top = V(cx + rx * math.cos(t), cy + d + rx * math.sin(t), 0)
    p_bot = V(cx + rx * math.cos(t), cy - d - rx * math.sin(t), 0)
    m = math.radians(90.0 + a0 / 2.0)
    edges = [
        cq.Edge.makeThreePointArc(
            p_top,
            V(cx + rx * math.cos(m), cy + d + rx * math.sin(m), 0),
            V(cx - rx, cy + d, 0),
        ),
    ]
    if d > 1e-6:
        edges.append(cq.Edge.makeLine(V(cx - rx, cy + d, 0), V(cx - rx, cy - d, 0)))
    edges.append(
        cq.Edge.makeThreePointArc(
            V(cx - rx, cy - d, 0),
            V(cx + rx * math.cos(-m), cy - d + rx * math.sin(-m), 0),
            p_bot,
        )
    )
    return cq.Wire.assembleEdges(edges)


def b_outline(x0, xt, xb, h):
    # closed centre-line of a filled "B": stem, narrow top bowl, wider bottom bowl
    V = cq.Vector
    r = h / 2.0
    edges = [
        cq.Edge.makeLine(V(x0, -h, 0), V(x0, h, 0)),
        cq.Edge.makeLine(V(x0, h, 0), V(xt, h, 0)),
        cq.Edge.makeThreePointArc(V(xt, h, 0), V(xt + r, h / 2.0, 0), V(xt, 0, 0)),
        cq.Edge.makeLine(V(xt, 0, 0), V(xb, 0, 0)),
        cq.Edge.makeThreePointArc(V(xb, 0, 0), V(xb + r, -h / 2.0, 0), V(xb, -h, 0)),
        cq.Edge.makeLine(V(xb, -h, 0), V(x0, -h, 0)),
    ]
    return cq.Wire.assembleEdges(edges)


h = CAP
s = STROKE / 2.0
letters = []
# N (diagonal a little heavier than the stems, as in a bold rounded face)
nx0, nx1 = 9.05 + s, 13.35 - s
letters.append((poly([(nx0, -h), (nx0, h)]), STROKE))
dn = (HEAVY - STROKE) / 2.0  # keep the heavier diagonal inside the cap height
letters.append((poly([(nx0, h - dn), (nx1, -h + dn)]), HEAVY))
letters.append((poly([(nx1, -h), (nx1, h)]), STROKE))
# Y  (arms meet a little above mid-height)
yx0, yx1 = 13.65 + HEAVY / 2.0, 18.85 - HEAVY / 2.0
ym = 16.2
yj = 0.75
ya = Y_ARM_TOP - HEAVY / 2.0  # arm tips reach above the cap height
letters.append((poly([(yx0, ya), (ym, yj)]), HEAVY))
letters.append((poly([(yx1, ya), (ym, yj)]), HEAVY))
letters.append((poly([(ym, yj), (ym, -h)]), STROKE + 0.05))
# B (filled, no counters)
bx0 = 18.95 + s
letters.append((b_outline(bx0, 21.1, 21.5, h), STROKE))
# I
letters.append((poly([(24.25, -h), (24.25, h)]), STROKE))
# C C
for cx in (C1_X, C1_X + C_PITCH):
    letters.append((c_wire(cx, 0.0, C_RX, C_RY, C_OPEN), STROKE))

# merge all strokes in 2D, extrude each glyph and round its top edge
faces = [stroke_face(w, wd) for w, wd in letters]
merged = faces[0].fuse(*faces[1:]).clean()
text_solids = []
for f in merged.Faces():
    g = cq.Workplane("XY").add(
        cq.Solid.extrudeLinear(f, cq.Vector(0, 0, TEXT_H + 0.05)).translate(
            cq.Vector(0, 0, THK - 0.05)
        )
    )
    try:
        g = g.faces(">Z").edges().fillet(TEXT_FILLET)
    except Exception:
        pass
    text_solids.append(g.val())

for t in text_solids:
    plate = plate.union(cq.Workplane("XY").add(t))


# ---------------- recessed logo (three swirl pockets) ----------------
# one swirl in polar coordinates (r normalised to LOGO_R, angle in degrees)
UNIT = [
    # outer edge along logo circle, counter-clockwise
    (0.93, 31.0), (0.985, 36.0), (1.0, 45.0), (1.0, 60.0), (1.0, 75.0),
    (1.0, 90.0), (1.0, 105.0), (1.0, 120.0), (1.0, 135.0), (0.985, 144.0),
    (0.93, 148.5),
    # back inwards: bump then down into the hook
    (0.87, 144.0), (0.80, 133.0), (0.70, 128.5), (0.58, 130.0),
    (0.45, 133.0), (0.32, 127.0), (0.235, 110.0), (0.225, 92.0),
    (0.27, 72.0), (0.36, 58.0), (0.47, 52.0), (0.58, 55.0),
    (0.65, 65.0), (0.70, 78.0), (0.725, 90.0), (0.74, 100.0),
    # blunt tongue tip
    (0.745, 104.5), (0.79, 106.5), (0.84, 105.0),
    # along the tongue's outer edge back to the band end
    (0.865, 99.0), (0.88, 88.0), (0.845, 74.0), (0.805, 61.0),
    (0.81, 48.0), (0.85, 38.0),
]


def logo_unit(rot):
    pts = []
    for r, a in UNIT:
        t = math.radians(a + rot)
        pts.append((coin_x + LOGO_DX + LOGO_R * r * math.cos(t), LOGO_DY + LOGO_R * r * math.sin(t)))
    return (
        cq.Workplane("XY", origin=(0, 0, THK - LOGO_DEPTH))
        .spline(pts, periodic=True)
        .close()
        .extrude(LOGO_DEPTH + 0.1)
    )


for k in range(3):
    plate = plate.cut(logo_unit(120.0 * k))

result = plate
